"""Hat-section cover / hood.

A channel running along Y with a closed end (+Y) and an open end (-Y),
bolting flanges along both sides (3 holes each, two relief pockets on the
underside of each flange), an inner bottom rabbet, a sliding-panel groove
just inside the open end, a -X roof round that widens toward the closed end
and a small corner gusset on the inside of the closed end.
"""
import math
import cadquery as cq

try:  # OCCT kernel bindings shipped with CadQuery (used for two niceties)
    from OCP.GC import GC_MakeSegment, GC_MakeArcOfCircle
    from OCP.GeomConvert import GeomConvert_CompCurveToBSplineCurve
    from OCP.gp import gp_Pnt
    from OCP.BRepBuilderAPI import BRepBuilderAPI_MakeEdge
    from OCP.BRepFeat import BRepFeat_SplitShape
    HAVE_OCP = True
except ImportError:  # pragma: no cover
    HAVE_OCP = False

# ---------------- driving dimensions (mm) ----------------
W = 200.0          # overall width across flanges (X)
D = 224.0          # overall length (Y)
H = 76.8           # overall height (Z)
T = 8.0            # shell thickness (walls and roof)
FL_W = 18.5        # flange width outside the wall
FL_T = 11.6        # flange thickness
NOTCH_W = 3.4      # inner bottom rabbet width
NOTCH_H = 6.2      # inner bottom rabbet height (walls / end wall bottom)
R_L0 = 26.5        # -X roof round: horizontal extent at the open (-Y) end
B_L0 = 23.6        #                vertical extent at the open end
R_L1 = 30.0        # -X roof round: horizontal extent at the closed (+Y) end
B_L1 = 25.2        #                vertical extent at the closed end
R_R = 30.0         # outer roof radius, +X side
END_T = 8.0        # closed end wall thickness (+Y end)
GR_Y0 = 4.5        # open end -> sliding-panel groove distance
GR_W = 6.0         # groove width (along Y)
GR_D = 2.7         # groove depth into walls / roof
CH_DX = 22.0       # corner gusset leg along the roof   (closed end, -X side)
CH_DZ = 18.4       # corner gusset leg down the wall
GUS_L = 4.0        # corner gusset length in front of the closed end
HOLE_D = 6.0       # flange hole diameter
HOLE_E = 8.0       # hole centre distance from flange outer edge
HOLE_Y = 9.0       # end hole centre distance from part ends
PK_W = 10.0        # underside pocket width (from flange inner edge outward)
PK_Y0 = 25.5       # pocket start measured from the nearer part end
PK_Y1 = 83.5       # pocket end measured from the nearer part end

VIEW = {"azimuth": 45, "elevation": 26}

# ---------------- derived values ----------------
xo = W / 2 - FL_W          # wall outer x
xi = xo - T                # wall inner x
xf = xi + NOTCH_W          # flange inner edge (start of the rabbet)
zt = H                     # roof top
zi = H - T                 # roof underside
rl_i = R_L0 - T            # inner -X round (elliptic) at the open end
bl_i = B_L0 - T
rr_i = R_R - T             # inner radius of the +X round
y_b = D / 2 - END_T        # inner face of the closed end wall


def arc_mid(cx, cz, r, a0, a1):
    """Mid point of an arc (angles in degrees) in the XZ plane."""
    a = math.radians((a0 + a1) / 2.0)
    return (cx + r * math.cos(a), cz + r * math.sin(a))


def at_y(wp_fn, y):
    """Draw a profile on an XZ workplane located at a given Y."""
    return wp_fn(cq.Workplane("XZ", origin=(0, y, 0)))


def wire_at(wp_fn, y):
    """Closed profile wire located in the XZ plane at a given Y."""
    w = at_y(wp_fn, y).val()
    assert isinstance(w, cq.Wire)
    return w


def outer_solid_plain():
    """Outer hat section (sharp -X roof corner) from a plain sketch."""
    wp = cq.Workplane("XZ", origin=(0, -D / 2, 0)).moveTo(-W / 2, 0)
    wp = wp.lineTo(W / 2, 0).lineTo(W / 2, FL_T).lineTo(xo, FL_T)
    wp = wp.lineTo(xo, zt - R_R)
    wp = wp.threePointArc(arc_mid(xo - R_R, zt - R_R, R_R, 0, 90),
                          (xo - R_R, zt))
    wp = wp.lineTo(-xo, zt).lineTo(-xo, FL_T).lineTo(-W / 2, FL_T).close()
    return wp.extrude(-D)


def outer_solid():
    """Outer hat section extruded along Y (sharp -X roof corner).
    The +X wall, the +X roof round and the roof form one smooth face
    (exact rational B-spline made from line + arc + line)."""
    if not HAVE_OCP:
        return outer_solid_plain()
    y = -D / 2
    c = math.radians(45.0)
    seg_w = GC_MakeSegment(gp_Pnt(xo, y, FL_T), gp_Pnt(xo, y, zt - R_R)).Value()
    arc = GC_MakeArcOfCircle(
        gp_Pnt(xo, y, zt - R_R),
        gp_Pnt(xo - R_R + R_R * math.cos(c), y, zt - R_R + R_R * math.sin(c)),
        gp_Pnt(xo - R_R, y, zt)).Value()
    seg_r = GC_MakeSegment(gp_Pnt(xo - R_R, y, zt), gp_Pnt(-xo, y, zt)).Value()
    comp = GeomConvert_CompCurveToBSplineCurve(seg_w)
    comp.Add(arc, 1e-7, True)
    comp.Add(seg_r, 1e-7, True)
    skin = cq.Edge(BRepBuilderAPI_MakeEdge(comp.BSplineCurve()).Edge())
    pts = [(-xo, zt), (-xo, FL_T), (-W / 2, FL_T), (-W / 2, 0.0),
           (W / 2, 0.0), (W / 2, FL_T), (xo, FL_T)]
    edges = [skin]
    for (x0, z0), (x1, z1) in zip(pts[:-1], pts[1:]):
        edges.append(cq.Edge.makeLine(cq.Vector(x0, y, z0),
                                      cq.Vector(x1, y, z1)))
    face = cq.Face.makeFromWires(cq.Wire.assembleEdges(edges))
    return cq.Workplane("XY").add(
        cq.Solid.extrudeLinear(face, cq.Vector(0, D, 0)))


def corner_cut(a, b):
    """Material outside the (elliptic) -X roof round with extents a x b."""
    def f(wp):
        wp = wp.moveTo(-xo + a, zt + 1.0).lineTo(-xo + a, zt)
        wp = wp.ellipseArc(a, b, 90, 180, sense=1, startAtCurrent=True)
        wp = wp.lineTo(-xo - 1.0, zt - b).lineTo(-xo - 1.0, zt + 1.0).close()
        return wp
    return f


def cavity(ri, bi):
    """Inner channel outline incl. the bottom rabbet; -X inner round ri x bi."""
    def f(wp):
        wp = wp.moveTo(-xf, -1.0).lineTo(xf, -1.0).lineTo(xf, NOTCH_H)
        wp = wp.lineTo(xi, NOTCH_H).lineTo(xi, zi - rr_i)
        wp = wp.threePointArc(arc_mid(xi - rr_i, zi - rr_i, rr_i, 0, 90),
                              (xi - rr_i, zi))
        wp = wp.lineTo(-xi + ri, zi)
        wp = wp.ellipseArc(ri, bi, 90, 180, sense=1, startAtCurrent=True)
        wp = wp.lineTo(-xi, NOTCH_H).lineTo(-xf, NOTCH_H).close()
        return wp
    return f


def groove_profile(wp):
    """Inner outline offset outward by the groove depth (walls + roof)."""
    ri = rl_i + GR_D
    bi = bl_i + GR_D
    rr = rr_i + GR_D
    xg = xi + GR_D
    zg = zi + GR_D
    wp = wp.moveTo(-xg, NOTCH_H - 1.0).lineTo(xg, NOTCH_H - 1.0)
    wp = wp.lineTo(xg, zi - rr_i)
    wp = wp.threePointArc(arc_mid(xi - rr_i, zi - rr_i, rr, 0, 90),
                          (xi - rr_i, zg))
    wp = wp.lineTo(-xi + rl_i, zg)
    wp = wp.ellipseArc(ri, bi, 90, 180, sense=1, startAtCurrent=True)
    return wp.close()


def gusset_profile(wp):
    return (wp.moveTo(-xi, zi - CH_DZ).lineTo(-xi + CH_DX, zi)
            .lineTo(-xi, zi).close())


# ---------------- build ----------------
# outer shell body
body = outer_solid()

# -X roof round whose radius grows from the open end to the closed end
corner = cq.Workplane("XY").add(cq.Solid.makeLoft(
    [wire_at(corner_cut(R_L0, B_L0), -D / 2 - 0.01),
     wire_at(corner_cut(R_L1, B_L1), D / 2 + 0.01)], True))
body = body.cut(corner)

# channel (constant wall thickness -> the -X inner round grows as well),
# stopping at the closed end wall
channel = cq.Workplane("XY").add(cq.Solid.makeLoft(
    [wire_at(cavity(R_L0 - T, B_L0 - T), -D / 2 - 0.01),
     wire_at(cavity(R_L1 - T, B_L1 - T), y_b)], True))
body = body.cut(channel)

# sliding-panel groove running around the inside near the open end
body = body.cut(at_y(groove_profile, -D / 2 + GR_Y0).extrude(-GR_W))

# corner gusset on the inside of the closed end (-X roof corner)
gusset = (at_y(gusset_profile, y_b - GUS_L).extrude(-(GUS_L + 0.01))
          .intersect(channel))
body = body.union(gusset)

# walls and end wall stand on the rabbet level, flanges reach the floor
body = body.cut(cq.Workplane("XY")
                .box(2 * xf, D + 2, NOTCH_H + 1, centered=(True, True, False))
                .translate((0, 0, -1.0)))

# underside relief pockets in the flanges (inner side, between the holes)
for sx in (-1, 1):
    for (y0, y1) in ((PK_Y0, PK_Y1), (D - PK_Y1, D - PK_Y0)):
        x_a = sx * xf
        x_b = sx * (xf + PK_W)
        pk = (cq.Workplane("XY")
              .box(PK_W, y1 - y0, NOTCH_H + 1, centered=False)
              .translate((min(x_a, x_b), -D / 2 + y0, -1.0)))
        body = body.cut(pk)

# flange bolt holes, 3 per side
pts = []
for sx in (-1, 1):
    for y in (-D / 2 + HOLE_Y, 0.0, D / 2 - HOLE_Y):
        pts.append((sx * (W / 2 - HOLE_E), y))
holes = (cq.Workplane("XY").pushPoints(pts)
         .circle(HOLE_D / 2).extrude(FL_T + 2).translate((0, 0, -1.0)))
body = body.cut(holes)



# ---------------- face seams of the -X roof round (cosmetic) ----------------
# The -X roof round is a separate (lofted) piece on the original part, so its
# end faces are bounded by seams: tangent lines across the open-end rim and
# a chord on the closed end.
def end_face(solid, y, sign):
    faces = [f for f in solid.Faces()
             if f.geomType() == "PLANE" and abs(f.Center().y - y) < 1e-3
             and f.normalAt().y * sign > 0.99]
    return max(faces, key=lambda f: f.Area())


def near_vertex(face, p):
    return min(face.Vertices(), key=lambda v: (v.Center() - cq.Vector(*p)).Length)


def add_seams(solid):
    f_open = end_face(solid, -D / 2, -1)
    f_closed = end_face(solid, D / 2, 1)
    sp = BRepFeat_SplitShape(solid.wrapped)
    # open end: tangent lines across the rim
    for p, q in (((-xo + R_L0, -D / 2, zt), (-xo + R_L0, -D / 2, zi)),
                 ((-xo, -D / 2, zt - B_L0), (-xi, -D / 2, zt - B_L0))):
        e = BRepBuilderAPI_MakeEdge(near_vertex(f_open, p).wrapped,
                                    near_vertex(f_open, q).wrapped).Edge()
        sp.Add(e, f_open.wrapped)
    # closed end: roof tangent -> inner wall line -> wall tangent
    v0 = near_vertex(f_closed, (-xo + R_L1, D / 2, zt)).Center()
    v2 = near_vertex(f_closed, (-xo, D / 2, zt - B_L1)).Center()
    v1 = cq.Vector(-xi, v2.y, v2.z)
    seam = cq.Wire.makePolygon([v0, v1, v2])
    sp.Add(seam.wrapped, f_closed.wrapped)
    sp.Build()
    out = cq.Shape.cast(sp.Shape()).Solids()
    if len(out) == 1 and out[0].isValid() and \
            abs(out[0].Volume() - solid.Volume()) < 1e-3 * solid.Volume():
        return out[0]
    return solid


if HAVE_OCP:
    try:
        body = cq.Workplane("XY").add(add_seams(body.val()))
    except Exception:
        pass

result = body
